import cadquery as cq

# =====================================================================
#  Open-top box with slide-lid grooves, hinge-rod knuckles, pin plate,
#  floor slots, front window + port and two side ports.
#  X = width, Y = length (front face at -L/2), Z = height.
# =====================================================================

# ---------------- overall size (mm) ----------------
W = 30.0        # width  (X)
L = 84.5        # length (Y)
H = 29.5        # height (Z)

# ---------------- outer edge treatment ----------------
C_FR = 5.0          # front-right vertical edge chamfer (45 deg)
FL_A = 4.9          # front-left corner, two-facet cut: run along X on the front face
FL_M = (1.25, 2.5)  # front-left corner crease (in from -X face, back from front face)
FL_B = 4.9          # front-left corner: run along Y on the -X face
C_BR = 2.4          # back-right vertical edge chamfer (45 deg)
C_BL = 2.8          # back-left corner: two-facet cut, run along each face
BL_M = 0.82         # back-left corner: crease offset from both faces
C_TOP = {-1: (2.7, 2.2), 1: (2.3, 2.6)}   # top outer chamfers of the side walls: (X run, Z run)
C_BOT = 2.2         # chamfer of the four bottom edges

# ---------------- walls / floors ----------------
T_SIDE = 2.2        # side wall thickness
T_FRONT = 3.5       # front wall thickness
T_BACK = 3.5        # back wall thickness
BACK_DROP = 2.6     # back wall top sits lower (lid slides in over it)
LABEL_TOP = 1.0     # shallow label recess on the back face: gap below the top
LABEL_H = 2.5       # label recess height
Z_FLOOR = 16.5      # floor of the front and back bays
Z_MID = 18.6        # top of the raised middle block
Z_SEAM = 24.0       # height of the seam line across the front face / back lip bottom

# thickened front part of the side walls with the lid groove
RAIL_T = 0.7        # extra thickness
RAIL_END = 17.6     # Y where the thickened part ends
GROOVE_TOP = 3.25   # groove upper edge below the top
GROOVE_H = 2.0      # groove height
GROOVE_D = 0.3      # groove depth

# hinge rods along the inner top edges
ROD_R = 1.15                    # front rods (on the thickened wall face)
ROD_FRONT_END = -L / 2 + 21.5   # front rods run from the front wall to here
BROD_R = 1.15                   # short rod stubs at the back corners
BROD_LEN = 3.6

# ---------------- front face openings ----------------
OV_CX = -0.5                    # barrel shaped window
OV_Z0, OV_Z1 = 19.2, 26.2
OV_HALF = 7.6
OV_BULGE = 1.1
OV_ARCH = 0.3

FP_CX, FP_CZ = -0.3, 8.9        # lower elliptical port
FP_A, FP_B = 7.2, 6.45
FCAV_DEPTH = 16.0               # cavity behind the front port
FBLK_SET = 2.5                  # set-back of the block inside that cavity
FBLK_X1 = 6.2                   # block right side

# ---------------- side ports ----------------
SP_Y_POS = 33.8                 # +X port centre (Y)
SP_Y_NEG = 22.6                 # -X port centre (Y)
SP_Z = 8.9
SP_D = 14.0
SLOT_W = 1.9                    # blind vertical slots above the ports
SLOT_Z0, SLOT_Z1 = 17.3, 25.3
SLOT_DEPTH_SIDE = 1.0
SLOT_PITCH = 3.3                # the -X side has two slots, +/- pitch

CH_Z0, CH_Z1 = 5.2, 13.1        # height band of the internal cavities
XC_Y0, XC_Y1 = 14.5, 38.4       # cross cavity joining both side ports

# ---------------- middle plate with pins ----------------
PLATE_HY = 9.05
PLATE_T = 0.4
PIN_D = 4.1
PIN_H = 1.8
PINS = [(-9.0, 5.9), (9.3, 5.7), (-1.4, 3.9),
        (-8.6, -6.1), (9.3, -6.2), (1.6, -4.3)]

# ---------------- floor slots ----------------
BACK_SLOTS_Y = [12.2, 17.3, 22.6, 28.0, 33.3]
BACK_SLOT_HX, BACK_SLOT_HY = 7.6, 1.15
FRAME_HX = 7.4                  # shallow frame recess around the back slots
FRAME_DEPTH = 0.4
FRAME_Y1 = 37.25
FRONT_SLOTS_Y = [-31.9, -26.6, -21.3, -15.9, -10.4]
FRONT_SLOT_LEN, FRONT_SLOT_W = 14.8, 2.5
SLOT_DEPTH = 1.2

hw, hl = W / 2, L / 2
X_IN = hw - T_SIDE              # inner face of the side walls
X_RAIL = X_IN - RAIL_T          # inner face of the thickened front part


def prism_xy(pts, z0=-1.0, h=H + 2.0):
    return cq.Workplane("XY").polyline(pts).close().extrude(h).translate((0, 0, z0))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# =====================================================================
# outer envelope
# =====================================================================
env = cq.Workplane("XY").box(W, L, H, centered=(True, True, False))
env = env.faces("<Z").edges().chamfer(C_BOT)

# top outer chamfers of the side walls (prisms along Y)
for sx in (-1, 1):
    tri = (cq.Workplane("XZ", origin=(0, hl + 1, 0))
           .polyline([(sx * (hw + 0.01), H - C_TOP[sx][1] - 0.01 * C_TOP[sx][1] / C_TOP[sx][0]),
                      (sx * (hw + 0.01), H + 0.01),
                      (sx * (hw - C_TOP[sx][0] - 0.01 * C_TOP[sx][0] / C_TOP[sx][1]), H + 0.01)])
           .close().extrude(L + 2))
    env = env.cut(tri)

# vertical corners
env = env.cut(prism_xy([(hw + 0.01, -hl - 0.01), (hw - C_FR, -hl - 0.01),
                        (hw + 0.01, -hl + C_FR)]))
env = env.cut(prism_xy([(-hw - 0.01, -hl - 0.01), (-hw + FL_A, -hl - 0.01),
                        (-hw + FL_M[0], -hl + FL_M[1]), (-hw - 0.01, -hl + FL_B)]))
env = env.cut(prism_xy([(hw + 0.01, hl + 0.01), (hw - C_BR, hl + 0.01), (hw + 0.01, hl - C_BR)]))
env = env.cut(prism_xy([(-hw - 0.01, hl + 0.01), (-hw + C_BL, hl + 0.01),
                        (-hw + BL_M, hl - BL_M), (-hw - 0.01, hl - C_BL)]))

body = env
# seam across the front face (upper part set back a hair)
body = body.cut(box(-hw + FL_A, hw - C_FR, -hl - 1, -hl + 0.05, Z_SEAM, H + 1))

# =====================================================================
# open top interior
# =====================================================================
body = body.cut(box(-X_IN, X_IN, -hl + T_FRONT, hl - T_BACK, Z_FLOOR, H + 1))
# lowered back wall
body = body.cut(box(-X_IN, X_IN, hl - T_BACK - 0.5, hl + 1, H - BACK_DROP, H + 1))

# thickened front part of the side walls, with the lid groove
for sx in (-1, 1):
    xa, xb = sorted((sx * (X_IN + 0.01), sx * X_RAIL))
    rail = box(xa, xb, -hl + T_FRONT - 0.01, RAIL_END, Z_FLOOR - 0.01, H)
    gx = sx * (X_RAIL + GROOVE_D)
    ga, gb = sorted((gx, sx * (X_RAIL - 0.5)))
    groove = box(ga, gb, -hl + T_FRONT - 0.02, RAIL_END + 0.02,
                 H - GROOVE_TOP - GROOVE_H, H - GROOVE_TOP)
    body = body.union(rail.cut(groove))

# =====================================================================
# hinge rods (clipped to the outer envelope)
# =====================================================================
rods = None
for sx in (-1, 1):
    rf = (cq.Workplane("XZ", origin=(0, ROD_FRONT_END, 0))
          .center(sx * X_RAIL, H - ROD_R).circle(ROD_R)
          .extrude(ROD_FRONT_END - (-hl + 1.0)))
    rb = (cq.Workplane("XZ", origin=(0, hl, 0))
          .center(sx * X_RAIL, H - BROD_R).circle(BROD_R)
          .extrude(BROD_LEN))
    rr = rf.union(rb)
    rods = rr if rods is None else rods.union(rr)
body = body.union(rods.intersect(env))

# =====================================================================
# front face: barrel window and elliptical port
# =====================================================================
x0, x1 = OV_CX - OV_HALF, OV_CX + OV_HALF
zm = 0.5 * (OV_Z0 + OV_Z1)
window = (cq.Workplane("XZ", origin=(0, -hl - 1, 0))
          .moveTo(x0, OV_Z0)
          .threePointArc((OV_CX, OV_Z0 - OV_ARCH), (x1, OV_Z0))
          .threePointArc((x1 + OV_BULGE, zm), (x1, OV_Z1))
          .threePointArc((OV_CX, OV_Z1 + OV_ARCH), (x0, OV_Z1))
          .threePointArc((x0 - OV_BULGE, zm), (x0, OV_Z0))
          .close()
          .extrude(-(T_FRONT + 2)))
body = body.cut(window)

port = (cq.Workplane("XZ", origin=(0, -hl - 1, 0))
        .center(FP_CX, FP_CZ).ellipse(FP_A, FP_B)
        .extrude(-(T_FRONT + 1.01)))
body = body.cut(port)
body = body.cut(box(FP_CX - FP_A, FP_CX + FP_A, -hl + T_FRONT - 0.01,
                    -hl + T_FRONT + FCAV_DEPTH, CH_Z0, CH_Z1))
body = body.union(box(FP_CX - FP_A, FBLK_X1, -hl + T_FRONT + FBLK_SET,
                      -hl + T_FRONT + FCAV_DEPTH + 0.01, CH_Z0 - 0.01, FP_CZ))

# =====================================================================
# side ports, cross cavity and blind slots
# =====================================================================
for sx, yc in ((1, SP_Y_POS), (-1, SP_Y_NEG)):
    body = body.cut(cq.Workplane("YZ", origin=(sx * (hw + 1), 0, 0))
                    .center(yc, SP_Z).circle(SP_D / 2)
                    .extrude(-sx * (T_SIDE + 1.2)))
body = body.cut(box(-X_IN - 0.01, X_IN + 0.01, XC_Y0, XC_Y1, CH_Z0, CH_Z1))

for sx, yc in ((1, SP_Y_POS + 0.2), (-1, SP_Y_NEG - SLOT_PITCH), (-1, SP_Y_NEG + SLOT_PITCH)):
    xo = sx * hw
    body = body.cut(box(min(xo, xo - sx * SLOT_DEPTH_SIDE) - (1 if sx < 0 else 0),
                        max(xo, xo - sx * SLOT_DEPTH_SIDE) + (1 if sx > 0 else 0),
                        yc - SLOT_W / 2, yc + SLOT_W / 2, SLOT_Z0, SLOT_Z1))

# =====================================================================
# back wall: inner lip and outer label recess
# =====================================================================
lip_hx = X_IN - 2 * BROD_R + 0.2
body = body.union(box(-lip_hx, lip_hx, hl - T_BACK - 0.7, hl - T_BACK + 0.01,
                      Z_SEAM, H - BACK_DROP))
lab_hx = hw - C_BL - 1.7
body = body.cut(box(-lab_hx, lab_hx, hl - 0.3, hl + 1, H - BACK_DROP - LABEL_TOP - LABEL_H,
                    H - BACK_DROP - LABEL_TOP))

# =====================================================================
# raised middle block, pin plate and pins
# =====================================================================
body = body.union(box(-X_RAIL - 0.01, X_RAIL + 0.01, -PLATE_HY, PLATE_HY, Z_FLOOR - 0.01, Z_MID))
body = body.union(box(-X_RAIL - 0.01, X_RAIL + 0.01, -PLATE_HY - 0.25, PLATE_HY + 0.25,
                      Z_MID - 0.01, Z_MID + PLATE_T))
body = body.union(cq.Workplane("XY", origin=(0, 0, Z_MID + PLATE_T - 0.01))
                  .pushPoints(PINS).circle(PIN_D / 2).extrude(PIN_H + 0.01))

# =====================================================================
# floor slots
# =====================================================================
body = body.cut(box(-FRAME_HX, FRAME_HX, PLATE_HY + 0.3, FRAME_Y1,
                    Z_FLOOR - FRAME_DEPTH, Z_FLOOR + 0.1))
for y in BACK_SLOTS_Y:
    body = body.cut(cq.Workplane("XY", origin=(0, y, Z_FLOOR - SLOT_DEPTH))
                    .ellipse(BACK_SLOT_HX, BACK_SLOT_HY).extrude(SLOT_DEPTH + 0.1))
body = body.cut(cq.Workplane("XY", origin=(0, 0, Z_FLOOR - SLOT_DEPTH))
                .pushPoints([(0, y) for y in FRONT_SLOTS_Y])
                .slot2D(FRONT_SLOT_LEN, FRONT_SLOT_W, 0).extrude(SLOT_DEPTH + 0.1))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
